import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------------------
# Laser-cut truss arm plate (flat plate in XY, thickness along Z)
# Origin: corner centre (big pivot hole) where long arm meets short arm.
# ---------------------------------------------------------------------------

T = 3.05            # plate thickness
W2 = 11.4           # half width of the long arm
W2S = 11.0          # half width of the short arm / link / eye
ANG_LONG = 22.0     # long arm direction (deg, measured from +X)
ANG_SHORT = -45.0   # short arm direction (deg)
ANG_END = 45.0      # direction of the left end section

# truss
NODE_PITCH = 30.1   # distance between nodes on one chord (long arm)
NODE_D0 = 30.3      # distance of the last far-side node from the corner
SHORT_PITCH = 30.25 # node pitch on the short arm
NODE_OFF = 6.0      # node rows offset from arm axis
N_LONG = 9          # nodes per chord on long arm
CHORD_IN = 5.7      # chord inner line (triangle base) offset from axis
TRI_HALF = 10.8     # half length of triangle base
END_GAP = 0.5       # gap between half triangle and end node line
HOLE_D = 2.9        # node hole diameter

# tabs on long arm edges
TAB_H = 2.8
TAB_L = 12.4
TAB_PITCH = 24.7
TAB_D0 = 277.1      # corner-side start of the first (left-most) tab
N_TABS = 12

# left end
V_DIST = 300.65     # distance from corner centre to virtual bend point
SMOOTH_NARROW = 0.5 # far edge of the bend is set in by this much
SMOOTH_L = 16.5     # from virtual bend point to end section start
END_L = 29.05       # length of the end section
END_EXTRA = 2.3     # end section extra width on the near side
END_TAB_H = 2.85
END_TAB_L = 7.0
END_TAB_PITCH = 14.5
NOTCH_R = 5.2
NOTCH_DEPTH = 1.5
NOTCH_OFF = 0.85    # notch centre offset from the end centreline (far side +)
END_SKEW = 1.1      # near side of the end face set back by this much

# corner / short arm / eye
CORNER_R = 15.0
BIG_HOLE_X = -1.45
BIG_HOLE_Y = 0.15
BIG_HOLE_D = 6.35
SIDE_HOLE_DX = 10.65
SHORT_I0 = 11.6     # first inner node of short arm
EYE_X = 64.0
EYE_Y = -99.8
EYE_HOLE_D = 11.8
OUT_BEND_R = 10.0
IN_BEND_R = 15.0


def add(p, q, s=1.0):
    return (p[0] + s * q[0], p[1] + s * q[1])


def unit(deg):
    r = math.radians(deg)
    return (math.cos(r), math.sin(r))


a = unit(ANG_LONG)              # along long arm (toward corner)
n = unit(ANG_LONG + 90)         # far side normal of long arm
b = unit(ANG_SHORT)             # along short arm (away from corner)
m = unit(ANG_SHORT + 90)        # outer side normal of short arm
a45 = unit(ANG_END)
n45 = unit(ANG_END + 90)


def LP(d, p):
    """point in long arm frame: d = distance from corner along -a, p = offset along n"""
    return (-d * a[0] + p * n[0], -d * a[1] + p * n[1])


def SP(s, q):
    """point in short arm frame"""
    return (s * b[0] + q * m[0], s * b[1] + q * m[1])


def line_int(p1, d1, p2, d2):
    """intersection of p1 + t d1 and p2 + u d2"""
    det = d1[0] * (-d2[1]) - d1[1] * (-d2[0])
    rx, ry = p2[0] - p1[0], p2[1] - p1[1]
    t = (rx * (-d2[1]) - ry * (-d2[0])) / det
    return (p1[0] + t * d1[0], p1[1] + t * d1[1])


def fillet_pts(p_in, corner, p_out, r):
    """fillet between line p_in->corner and corner->p_out; returns (t1, mid, t2)"""
    u1 = (corner[0] - p_in[0], corner[1] - p_in[1])
    l1 = math.hypot(*u1)
    u1 = (u1[0] / l1, u1[1] / l1)
    u2 = (p_out[0] - corner[0], p_out[1] - corner[1])
    l2 = math.hypot(*u2)
    u2 = (u2[0] / l2, u2[1] / l2)
    cosang = -(u1[0] * u2[0] + u1[1] * u2[1])
    half = math.acos(max(-1.0, min(1.0, cosang))) / 2.0
    tl = r / math.tan(half)
    t1 = (corner[0] - u1[0] * tl, corner[1] - u1[1] * tl)
    t2 = (corner[0] + u2[0] * tl, corner[1] + u2[1] * tl)
    bis = (u2[0] - u1[0], u2[1] - u1[1])
    lb = math.hypot(*bis)
    bis = (bis[0] / lb, bis[1] / lb)
    dc = r / math.sin(half)
    c = (corner[0] + bis[0] * dc, corner[1] + bis[1] * dc)
    mid = (c[0] - bis[0] * r, c[1] - bis[1] * r)
    return t1, mid, t2


# ---------------------------------------------------------------- outline
segs = []   # ("L", pt) line | ("A", mid, end) arc | ("S", end, t0, t1) tangent spline


def L(p):
    segs.append(("L", p))


def A(mid, end):
    segs.append(("A", mid, end))


E = (EYE_X, EYE_Y)
start = (EYE_X + W2S, EYE_Y)

# link right edge -> outer bend
o_link = (EYE_X + W2S, 0.0)
o_short = SP(0.0, W2S)
ob = line_int(o_link, (0, 1), o_short, b)
t1, mid, t2 = fillet_pts(start, ob, o_short, OUT_BEND_R)
L(t1)
A(mid, t2)

# short arm outer edge -> outer corner fillet
far_line_pt = LP(0.0, W2)
oc = line_int(o_short, b, far_line_pt, a)
t1, mid, t2 = fillet_pts(t2, oc, LP(50.0, W2), CORNER_R)
L(t1)
A(mid, t2)

# far edge with tabs (going away from corner)
tabs = [(TAB_D0 - k * TAB_PITCH, TAB_D0 - k * TAB_PITCH + TAB_L) for k in range(N_TABS)]
tabs.sort()
for d0, d1 in tabs:
    L(LP(d0, W2))
    L(LP(d0, W2 + TAB_H))
    L(LP(d1, W2 + TAB_H))
    L(LP(d1, W2))

# left bend: the 45 deg end part's centre line crosses the long arm axis at V
V = LP(V_DIST, 0.0)
first_tab_end = max(t[1] for t in tabs)


def EP(s, q):
    """end frame: s = distance from V along -a45, q = offset along n45"""
    return (V[0] - s * a45[0] + q * n45[0], V[1] - s * a45[1] + q * n45[1])


# far edge: arc tangent to the long arm far edge at the first tab and to the
# (slightly narrower) far edge of the 45 deg part
T1 = LP(first_tab_end, W2)
K = line_int(T1, (-a[0], -a[1]), EP(0.0, W2 - SMOOTH_NARROW), (-a45[0], -a45[1]))
tlf = math.hypot(K[0] - T1[0], K[1] - T1[1])
turn = math.radians(ANG_END - ANG_LONG)
r_far = tlf / math.tan(turn / 2)
t1, mid, t2 = fillet_pts(T1, K, add(K, a45, -2 * tlf), r_far)
A(mid, t2)
L(EP(SMOOTH_L, W2 - SMOOTH_NARROW))
L(EP(SMOOTH_L, W2))


s_end = SMOOTH_L + END_L
# far edge of end section (flush) with tabs; tabs measured from end face
etabs = [(s_end - END_TAB_PITCH - END_TAB_L, s_end - END_TAB_PITCH),
         (s_end - END_TAB_L, s_end)]
for s0, s1 in etabs:
    L(EP(s0, W2))
    L(EP(s0, W2 + END_TAB_H))
    L(EP(s1, W2 + END_TAB_H))
    if s1 != s_end:
        L(EP(s1, W2))
# end face (slightly skewed: near side shorter by END_SKEW) with a shallow notch
qnear = -(W2 + END_EXTRA)
q_far, q_nr = W2 + END_TAB_H, qnear - END_TAB_H


def end_s(q):
    return s_end - END_SKEW * (q_far - q) / (q_far - q_nr)


hc = math.sqrt(NOTCH_R ** 2 - (NOTCH_R - NOTCH_DEPTH) ** 2)
qn = NOTCH_OFF
L(EP(end_s(qn + hc), qn + hc))
A(EP(end_s(qn) - NOTCH_DEPTH, qn), EP(end_s(qn - hc), qn - hc))
L(EP(end_s(q_nr), q_nr))
for s1, s0 in [(etabs[1][1], etabs[1][0]), (etabs[0][1], etabs[0][0])]:
    s1 -= END_SKEW
    s0 -= END_SKEW
    if s1 != s_end - END_SKEW:
        L(EP(s1, qnear))
        L(EP(s1, qnear - END_TAB_H))
    L(EP(s0, qnear - END_TAB_H))
    L(EP(s0, qnear))
L(EP(SMOOTH_L - END_SKEW / 2, qnear))
L(EP(SMOOTH_L - END_SKEW / 2, -W2))

# near edge of bend: one smooth transition curve from the step to the first tab
segs.append(("S", LP(first_tab_end, -W2), a45, a))

# near edge with tabs toward corner; last tab merges into short arm inner edge
i_short = SP(0.0, -W2S)
for idx, (d0, d1) in enumerate(sorted(tabs, reverse=True)):
    L(LP(d1, -W2))
    L(LP(d1, -W2 - TAB_H))
    if idx < len(tabs) - 1:
        L(LP(d0, -W2 - TAB_H))
        L(LP(d0, -W2))
    else:
        ic = line_int(LP(d1, -W2 - TAB_H), a, i_short, b)
        L(ic)

# inner bend to link left edge
i_link = (EYE_X - W2S, 0.0)
ib = line_int(i_short, b, i_link, (0, 1))
t1, mid, t2 = fillet_pts(ic, ib, (EYE_X - W2S, EYE_Y), IN_BEND_R)
L(t1)
A(mid, t2)
L((EYE_X - W2S, EYE_Y))
A((EYE_X, EYE_Y - W2S), start)

# build wire
wp = cq.Workplane("XY").moveTo(*start)
cur = start
for s in segs:
    if s[0] == "L":
        if math.hypot(s[1][0] - cur[0], s[1][1] - cur[1]) < 1e-6:
            continue
        wp = wp.lineTo(*s[1])
        cur = s[1]
    elif s[0] == "A":
        wp = wp.threePointArc(s[1], s[2])
        cur = s[2]
    else:
        wp = wp.spline([s[1]], tangents=[s[2], s[3]], includeCurrent=True)
        cur = s[1]
plate = wp.close().extrude(T)

# ---------------------------------------------------------------- holes
def through(wp2d):
    """extrude a 2D sketch as a through-cutter (a little longer than the plate)"""
    return wp2d.extrude(T + 2.0)


def dT(i):
    """distance of far-side node i (0 = left-most) from the corner"""
    return NODE_D0 + NODE_PITCH * (N_LONG - 1 - i)


holes = []

for i in range(N_LONG):
    holes.append(LP(dT(i), NODE_OFF))
    holes.append(LP(dT(i) - NODE_PITCH / 2, -NODE_OFF))
for j in range(3):
    holes.append(SP(SHORT_I0 + SHORT_PITCH * j, -NODE_OFF))
for j in range(2):
    holes.append(SP(SHORT_I0 + SHORT_PITCH * (j + 0.5), NODE_OFF))
holes.append((BIG_HOLE_X - SIDE_HOLE_DX, BIG_HOLE_Y))
holes.append((BIG_HOLE_X + SIDE_HOLE_DX, BIG_HOLE_Y))

base = cq.Workplane("XY").workplane(offset=-1.0)
plate = plate.cut(through(base.pushPoints(holes).circle(HOLE_D / 2)))
plate = plate.cut(through(base.center(BIG_HOLE_X, BIG_HOLE_Y).circle(BIG_HOLE_D / 2)))
plate = plate.cut(through(base.center(*E).circle(EYE_HOLE_D / 2)))

# ---------------------------------------------------------------- truss cut-outs
half_base = TRI_HALF


def tri(frame, c, sgn, part="full", pitch=NODE_PITCH):
    """triangle cut-out with its apex toward the node at (c, sgn*NODE_OFF) and its
    base on the opposite chord line (-sgn*CHORD_IN); sides parallel to the truss
    diagonals.  part = "lo"/"hi" gives the half on the smaller/larger s side.
    frame(s, q) maps to XY."""
    slope = (2 * NODE_OFF) / (pitch / 2.0)       # diagonal member slope
    apex_off = half_base * slope - CHORD_IN      # apex distance from axis
    ap = (c, sgn * apex_off)
    b1 = (c - half_base, -sgn * CHORD_IN)
    b2 = (c + half_base, -sgn * CHORD_IN)
    if part == "full":
        pts = [b1, b2, ap]
    elif part == "lo":      # half with s < c
        f = (apex_off + CHORD_IN)
        cut = c - END_GAP
        k = (c - cut) / half_base
        pts = [b1, (cut, -sgn * CHORD_IN), (cut, sgn * apex_off - sgn * f * k)]
    else:                   # half with s > c
        f = (apex_off + CHORD_IN)
        cut = c + END_GAP
        k = (cut - c) / half_base
        pts = [(cut, -sgn * CHORD_IN), b2, (cut, sgn * apex_off - sgn * f * k)]
    return [frame(*p) for p in pts]


cut_polys = []
# long arm: s = distance from corner (d)
for i in range(N_LONG):
    dt = dT(i)
    db = dt - NODE_PITCH / 2
    if i == 0:
        cut_polys.append(tri(LP, dt, +1, "lo"))
    else:
        cut_polys.append(tri(LP, dt, +1))
    if i == N_LONG - 1:
        cut_polys.append(tri(LP, db, -1, "hi"))
    else:
        cut_polys.append(tri(LP, db, -1))
# short arm
sI = [SHORT_I0 + SHORT_PITCH * j for j in range(3)]
sO = [SHORT_I0 + SHORT_PITCH * (j + 0.5) for j in range(2)]
cut_polys.append(tri(SP, sI[0], -1, "hi", SHORT_PITCH))
cut_polys.append(tri(SP, sO[0], +1, "full", SHORT_PITCH))
cut_polys.append(tri(SP, sI[1], -1, "full", SHORT_PITCH))
cut_polys.append(tri(SP, sO[1], +1, "full", SHORT_PITCH))
cut_polys.append(tri(SP, sI[2], -1, "lo", SHORT_PITCH))

cutter = None
for poly in cut_polys:
    c = through(base.polyline(poly).close())
    cutter = c if cutter is None else cutter.union(c)
plate = plate.cut(cutter)

result = plate
